import math
import cadquery as cq

# ============================================================ parameters
# ---- base (world frame, Z up) -------------------------------------------
FLANGE_D = 120.0
FLANGE_T = 5.0
FLANGE_HOLE_PCD_R = 54.3
FLANGE_HOLE_D = 4.0
FLANGE_HOLE_ROT = 4.0          # deg, rotation of the 4-hole pattern
BASE_D = 96.0
BASE_H = 58.0                  # top of the turntable housing
BASE_WALL = 4.0
BASE_CAV_H = 39.0              # depth of the open underside cavity
BASE_POCKET_Z = 20.0           # bottom of the flat pocket in the rear wall
SIDE_HOLE_D = 10.0
SIDE_HOLE_Z = 13.5
SIDE_HOLE_ANG = -41.0          # deg, direction of the cable hole
BASE_SEAM_ANG = 45.0           # deg, where the cylinder seams sit (out of sight)

# ---- arm (local frame: x in arm plane, y along the joint axes, z up) -----
# the whole arm is rotated ARM_ROT about Z into the world
ARM_ROT = 45.0
ARM_X = 15.0                   # offset of the arm plane from the base axis
SHOULDER_Z = 96.0
ELBOW_Z = 216.0
CUP_R = 21.5                   # joint cup (dome) radius
CUP_Y0, CUP_Y1 = -9.0, 3.5     # upper arm extent along the joint axis
CUP_SPH_Y = -0.5               # centre of the domed cups along y
CUP_RECESS = 7.0               # depth of the recessed cup face
CUP_FACE_R = 17.5
LINK_WAIST = 31.0
LINK_ROUND = 7.5               # edge round of the upper arm link
LINK_Y1 = 7.5                  # back face of the upper arm link

BRK_Y0, BRK_Y1 = 8.0, 22.0     # shoulder bracket extent along the joint axis
BRK_LEFT_X = -35.0
BRK_LEFT_H = 16.0              # height of the short vertical rear edge
BRK_TOP_X = 0.5                # end of the flat crown on the slanted side
BRK_R = 23.0                   # radius of the bracket crown about the shoulder axis

FA_W = 38.0                    # forearm width (x)
FA_Y0, FA_Y1 = 4.0, 23.0       # forearm extent along y
FA_TOP = 356.5
FA_BANDS = (257.0, 305.0)      # z of the sleeve joints on the forearm
FA_CHANNEL_L = (263.0, 315.0)  # cable channel on the -x side
FA_CHANNEL_R = (251.0, 313.0)  # cable channel on the +x side
WRIST_Z = 345.5

GRIP_TILT = 16.0               # deg, gripper pitch (nose up)
GRIP_ROOT_X = -4.0
GRIP_VC = 2.5                  # gripper centre line (y)


def rot_arm(shape):
    return shape.rotate((0, 0, 0), (0, 0, 1), ARM_ROT)


def xz_plane(y):
    """Workplane at y whose local (x, y) are arm-local (x, z); extrudes toward -y."""
    return cq.Workplane(cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))


# ============================================================ base
def make_base():
    flange = cq.Workplane("XY").circle(FLANGE_D / 2).extrude(FLANGE_T)
    body = cq.Workplane("XY").circle(BASE_D / 2).extrude(BASE_H)
    base = flange.union(body)
    try:
        base = base.faces(">Z").edges().fillet(1.0)
    except Exception:
        pass
    # keep the cylinder seams on the rear side
    base = base.rotate((0, 0, 0), (0, 0, 1), BASE_SEAM_ANG)
    # open underside cavity
    base = base.cut(cq.Workplane("XY").circle(BASE_D / 2 - BASE_WALL).extrude(BASE_CAV_H)
                    .rotate((0, 0, 0), (0, 0, 1), BASE_SEAM_ANG))
    # flange holes (with a small counterbore)
    pts = []
    for i in range(4):
        a = math.radians(FLANGE_HOLE_ROT + 90 * i)
        pts.append((FLANGE_HOLE_PCD_R * math.cos(a), FLANGE_HOLE_PCD_R * math.sin(a)))
    base = base.cut(cq.Workplane("XY").pushPoints(pts).circle(FLANGE_HOLE_D / 2).extrude(FLANGE_T))
    base = base.cut(cq.Workplane("XY").workplane(offset=FLANGE_T - 0.8)
                    .pushPoints(pts).circle(FLANGE_HOLE_D / 2 + 1.2).extrude(1.0))
    # shallow parting groove below the lid
    groove = (cq.Workplane("XY").workplane(offset=BASE_H - 3.2)
              .circle(BASE_D / 2 + 1).circle(BASE_D / 2 - 0.6).extrude(0.8)
              .rotate((0, 0, 0), (0, 0, 1), BASE_SEAM_ANG))
    base = base.cut(groove)
    # cable hole in the side wall with a grommet bar
    a = math.radians(SIDE_HOLE_ANG)
    d = (math.cos(a), math.sin(a), 0)
    pl = cq.Plane(origin=(0, 0, SIDE_HOLE_Z), xDir=(-d[1], d[0], 0), normal=d)
    base = base.cut(cq.Workplane(pl).circle(SIDE_HOLE_D / 2).extrude(BASE_D))
    grom = (cq.Workplane(pl).workplane(offset=BASE_D / 2 - BASE_WALL)
            .center(0, 0.8).rect(SIDE_HOLE_D, 2.0).extrude(BASE_WALL - 0.8))
    base = base.union(grom)
    # flat pocket on the rear inner wall and an oval bearing ring on the ceiling
    pocket = (cq.Workplane("XY").box(30, 12, BASE_CAV_H - BASE_POCKET_Z)
              .translate((2.0, BASE_D / 2 - BASE_WALL - 8.0, 0.5 * (BASE_CAV_H + BASE_POCKET_Z))))
    ring = (cq.Workplane("XY").workplane(offset=BASE_CAV_H - 2.5)
            .center(2, 26).slot2D(34, 11, 0).extrude(3.0))
    ring = ring.cut(cq.Workplane("XY").workplane(offset=BASE_CAV_H - 2.5)
                    .center(2, 26).slot2D(30, 7, 0).extrude(3.0))
    base = base.cut(rot_arm(pocket)).union(rot_arm(ring))
    return base


# ============================================================ shoulder bracket
def make_bracket():
    cx, cz = ARM_X, SHOULDER_Z
    R = BRK_R
    top = cz + R
    z0 = BASE_H - 0.5
    a0 = math.radians(-60)
    a1 = math.radians(20)
    prof = (xz_plane(BRK_Y1)
            .moveTo(BRK_LEFT_X, z0)
            .lineTo(cx + R * math.cos(a0), z0)
            .lineTo(cx + R * math.cos(a0), cz + R * math.sin(a0))
            .threePointArc((cx + R * math.cos(a1), cz + R * math.sin(a1)), (cx, top))
            .lineTo(BRK_TOP_X, top)
            .lineTo(BRK_LEFT_X, z0 + BRK_LEFT_H)
            .close()
            .extrude(BRK_Y1 - BRK_Y0))
    ym = 0.5 * (BRK_Y0 + BRK_Y1)
    for pt, rad in (((BRK_TOP_X, ym, top), 14.0), ((BRK_LEFT_X, ym, z0 + BRK_LEFT_H), 8.0)):
        try:
            prof = prof.edges(cq.selectors.NearestToPointSelector(pt)).fillet(rad)
        except Exception:
            pass
    try:
        prof = prof.faces("<Y").edges().fillet(0.8)
    except Exception:
        pass
    # servo housing pad on the back side
    pad = (xz_plane(BRK_Y1 + 2.5)
           .center(cx - 15, cz - 12)
           .transformed(rotate=(0, 0, 55))
           .rect(44, 24).extrude(2.5))
    pad = pad.edges("|Y").fillet(6)
    srv = (xz_plane(BRK_Y1 + 4.5).center(cx - 15, cz - 12).transformed(rotate=(0, 0, 55))
           .center(-4, 0).rect(24, 14).extrude(2.0))
    horn = xz_plane(BRK_Y1 + 5.5).center(cx, cz).circle(5).extrude(3.5)
    prof = prof.union(pad).union(srv).union(horn)
    # shoulder hub joining the bracket and the upper arm
    hub = xz_plane(BRK_Y0 + 2).center(cx, cz).circle(9).extrude(BRK_Y0 + 2 - (CUP_Y1 - 1))
    return prof.union(hub)


# ============================================================ upper arm
def make_upper_arm():
    cx = ARM_X
    r = CUP_R
    a = math.radians(25)
    zm = 0.5 * (SHOULDER_Z + ELBOW_Z)
    w = LINK_WAIST / 2
    ly0 = CUP_Y0 + 0.5
    link = (xz_plane(LINK_Y1)
            .moveTo(cx + r * math.cos(a), SHOULDER_Z + r * math.sin(a))
            .threePointArc((cx + w, zm), (cx + r * math.cos(a), ELBOW_Z - r * math.sin(a)))
            .lineTo(cx - r * math.cos(a), ELBOW_Z - r * math.sin(a))
            .threePointArc((cx - w, zm), (cx - r * math.cos(a), SHOULDER_Z + r * math.sin(a)))
            .close()
            .extrude(LINK_Y1 - ly0))
    try:
        link = link.faces("<Y or >Y").edges().fillet(LINK_ROUND)
    except Exception:
        try:
            link = link.faces("<Y").edges().fillet(LINK_ROUND)
        except Exception:
            pass
    # domed joint cups: sphere about the joint centre clipped by the arm faces
    slab = cq.Workplane("XY").box(4 * r, CUP_Y1 - CUP_Y0, 4 * r).translate((cx, 0.5 * (CUP_Y0 + CUP_Y1), 0))
    arm = link
    for zc in (SHOULDER_Z, ELBOW_Z):
        sph = cq.Workplane("XY").sphere(r).translate((cx, CUP_SPH_Y, zc))
        arm = arm.union(sph.intersect(slab.translate((0, 0, zc))))
    # recessed cup faces and holes
    joints = [(cx, SHOULDER_Z), (cx, ELBOW_Z)]
    yf = CUP_Y0 + CUP_RECESS
    arm = arm.cut(xz_plane(yf).pushPoints(joints).circle(CUP_FACE_R).extrude(CUP_RECESS + 1))
    arm = arm.cut(xz_plane(yf + 6).pushPoints(joints).circle(3.75).extrude(8))
    small = []
    for zc in (SHOULDER_Z, ELBOW_Z):
        small += [(cx, zc + 7.3), (cx, zc - 7.3)]
    arm = arm.cut(xz_plane(yf + 4).pushPoints(small).circle(1.5).extrude(6))
    face_r = CUP_FACE_R
    # notch in the elbow cup rim
    notch = xz_plane(CUP_Y0 + 3.0).center(cx, ELBOW_Z - face_r - 0.5).ellipse(5, 3).extrude(5)
    arm = arm.cut(notch)
    # screw stub on the shoulder cup rim
    ang = math.radians(228)
    dvec = (math.cos(ang), 0, math.sin(ang))
    rs = r - 5.0
    stub = (cq.Workplane(cq.Plane(origin=(cx + rs * dvec[0], CUP_Y0 + 5.0, SHOULDER_Z + rs * dvec[2]),
                                  xDir=(0, 1, 0), normal=dvec))
            .circle(3.0).extrude(9.0))
    arm = arm.union(stub)
    # elbow hub joining the upper arm and the forearm
    hub = xz_plane(FA_Y0 + 2).center(cx, ELBOW_Z).circle(9).extrude(4)
    return arm.union(hub)


# ============================================================ forearm
def make_forearm():
    cx = ARM_X
    t = FA_Y1 - FA_Y0
    hw = FA_W / 2
    ym = 0.5 * (FA_Y0 + FA_Y1)
    body = (xz_plane(FA_Y1)
            .moveTo(cx - hw, FA_TOP)
            .lineTo(cx - hw, ELBOW_Z)
            .threePointArc((cx, ELBOW_Z - hw), (cx + hw, ELBOW_Z))
            .lineTo(cx + hw, FA_TOP)
            .close()
            .extrude(t))
    try:
        body = body.edges("|Z").fillet(2.0)
    except Exception:
        pass
    # sleeve joints: a thin groove below, a recessed slot above
    zlo, zhi = FA_BANDS
    body = body.cut(cq.Workplane("XY").box(FA_W + 4, 2.0, 1.2).translate((cx, FA_Y0, zlo)))
    for sx in (-1, 1):
        body = body.cut(cq.Workplane("XY").box(2.0, 8.0, 1.2).translate((cx + sx * hw, FA_Y0 + 3.0, zlo)))
    body = body.cut(xz_plane(FA_Y0 + 1.5).center(cx, zhi).slot2D(FA_W - 8, 3.2, 0).extrude(2.0))
    body = body.cut(cq.Workplane("XY").box(FA_W + 4, 2.0, 0.8).translate((cx, FA_Y0, zhi)))
    # slightly waisted sleeve between the joints
    L = zhi - zlo
    sag = 1.0
    Rw = (L * L / 4 + sag * sag) / (2 * sag)
    for sx in (-1, 1):
        cutter = (xz_plane(FA_Y1 + 1).center(cx + sx * (hw + Rw - sag), 0.5 * (zlo + zhi))
                  .circle(Rw).extrude(t + 2))
        band = cq.Workplane("XY").box(FA_W + 10, t + 4, L).translate((cx, ym, 0.5 * (zlo + zhi)))
        body = body.cut(cutter.intersect(band))
    # cable channels on both narrow sides
    for sx, (c0, c1) in ((-1, FA_CHANNEL_L), (1, FA_CHANNEL_R)):
        zc, L = 0.5 * (c0 + c1), c1 - c0
        body = body.cut(cq.Workplane("XY").box(4, 7, L).translate((cx + sx * hw, ym, zc)))
        body = body.union(cq.Workplane("XY").box(2.5, 4, L - 6).translate((cx + sx * (hw - 1.2), ym, zc)))
    # raised corner lips of the wrist bracket
    for sx in (-1, 1):
        lip = cq.Workplane("XY").box(3.5, t, 2.0).translate((cx + sx * (hw - 1.75), ym, FA_TOP + 0.9))
        body = body.union(lip)
    # servo covers on the back face (wrist and elbow)
    for zs, L, W, hz, rz, rh in ((FA_TOP - 27, 52, 28, 18, -3, 22), (ELBOW_Z + 14.5, 54, 32, -7.5, 0, 30)):
        pad = xz_plane(FA_Y1 + 2.0).center(cx, zs).slot2D(L, W, 90).extrude(2.2)
        rim = xz_plane(FA_Y1 + 2.2).center(cx, zs).slot2D(L - 4, W - 4, 90).extrude(0.8)
        pocket = xz_plane(FA_Y1 + 2.8).center(cx, zs + rz).rect(W - 11, rh).extrude(1.8)
        horn = xz_plane(FA_Y1 + 2.6).center(cx, zs + hz).circle(4.5).extrude(2.4)
        body = body.union(pad).cut(rim).cut(pocket).union(horn)
    return body


# ============================================================ wrist tongue
def make_tongue():
    y0 = FA_Y0 - 3.5
    cx = ARM_X
    R = 10.5
    tg = (xz_plane(y0 + 3.6)
          .moveTo(GRIP_ROOT_X - 6, WRIST_Z + 4)
          .lineTo(cx - 2, WRIST_Z + R)
          .threePointArc((cx + R, WRIST_Z), (cx - 2, WRIST_Z - R))
          .lineTo(GRIP_ROOT_X - 6, WRIST_Z - 4)
          .close()
          .extrude(3.6))
    slot = xz_plane(y0 + 5).center(cx, WRIST_Z).slot2D(7, 3.6, 10).extrude(6)
    return tg.cut(slot)


# ============================================================ gripper
def grip_plane(w_off):
    """plane tilted by GRIP_TILT; local x = +y (lateral v), local y = along the fingers (u)."""
    s, c = math.sin(math.radians(GRIP_TILT)), math.cos(math.radians(GRIP_TILT))
    nrm = (s, 0, c)
    org = (GRIP_ROOT_X + w_off * s, 0.0, WRIST_Z + w_off * c)
    return cq.Workplane(cq.Plane(origin=org, xDir=(0, 1, 0), normal=nrm))


def bar(p0, p1, half_w, w_off, th):
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    return (grip_plane(w_off).center(0.5 * (p0[0] + p1[0]), 0.5 * (p0[1] + p1[1]))
            .slot2D(L + 2 * half_w, 2 * half_w, ang).extrude(th))


def make_gripper():
    vc = GRIP_VC
    # gripper servo body with its horn
    g = grip_plane(-3.0).center(vc + 12.5, 9.0).rect(15, 18).extrude(12.0)
    g = g.union(grip_plane(9.0).center(vc + 13, 8.0).circle(4.5).extrude(1.2))
    # holder frame (window plate) on the front side of the servo
    fr = grip_plane(3.0).center(vc + 4.0, 13.0).rect(3.0, 10.0).extrude(10.0)
    fr = fr.cut(grip_plane(5.5).center(vc + 4.0, 13.0).rect(4, 5.0).extrude(5.0))
    g = g.union(fr)
    # base plate carrying the finger links
    g = g.union(grip_plane(-3.0).center(vc, 10.0).rect(20, 18).extrude(3.0))
    pins = []
    for sv in (-1, 1):
        B1 = (vc + sv * 3.5, 18.5)
        B2 = (vc + sv * 6.0, 4.5)
        C1 = (vc + sv * 12.0, 38.0)
        C2 = (vc + sv * 15.5, 24.0)
        claw = (grip_plane(-1.0)
                .moveTo(vc + sv * 17.0, 22.0)
                .lineTo(*C1)
                .threePointArc((vc + sv * 11.8, 52.0), (vc + sv * 8.5, 63.5))
                .offset2D(3.2).extrude(5.0))
        g = g.union(claw)
        g = g.union(bar(B1, C1, 3.0, 3.8, 2.2))
        g = g.union(bar(B2, C2, 3.0, 3.8, 2.2))
        pins += [B1, B2, C1, C2]
    g = g.union(grip_plane(-3.5).pushPoints(pins).circle(1.9).extrude(11.0))
    g = g.union(grip_plane(-3.5).pushPoints(pins).circle(2.8).extrude(0.8))
    g = g.union(grip_plane(6.0).pushPoints(pins).circle(2.6).extrude(1.5))
    return g


# ============================================================ turntable details
def make_top_details():
    # small cable clip on the turntable
    tab = cq.Workplane("XY").box(6.0, 11.0, 12.5).translate((-20.5, -4.0, BASE_H + 6.25 - 0.5))
    tab = tab.edges("|X and >Z").fillet(2.5)
    tab = tab.cut(cq.Workplane("XY").box(10, 5, 5).translate((-20.5, -4.0, BASE_H + 5.5)))
    return tab


def build():
    base = make_base()
    arm = (make_bracket()
           .union(make_upper_arm())
           .union(make_forearm())
           .union(make_tongue())
           .union(make_gripper())
           .union(make_top_details()))
    res = base.union(rot_arm(arm))
    # screw holes on the turntable in front of the bracket
    holes = (cq.Workplane("XY").workplane(offset=BASE_H - 2)
             .pushPoints([(-6, 0.5), (6, 0.5)]).circle(0.9).extrude(3))
    res = res.cut(rot_arm(holes))
    return res


result = build()
